import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# =====================================================================
#  Open-top electronics project box
#  - rectangular tub, rounded vertical outer corners, sharp inner cavity
#  - +X wall : rectangular switch slot, large round hole, small round hole
#  - -X wall : row of four small (LED) holes
#  - floor   : six blind mounting holes for PCBs
# =====================================================================

# ---------------- overall body ----------------
W = 65.0          # outer width  (X)
L = 100.0         # outer length (Y)
H = 39.2          # outer height (Z)
T = 4.2           # side wall thickness
R_OUT = 4.0       # outer vertical corner radius
T_FLOOR = 4.5     # floor thickness

# ---------------- +X wall features ----------------
# positions: Y from box centre, Z from the underside
SLOT_Y0, SLOT_Y1 = -33.9, -22.4     # rectangular slot, Y extent
SLOT_Z0, SLOT_Z1 = 12.6, 30.9       # rectangular slot, Z extent
BIG_D, BIG_Y, BIG_Z = 9.1, 0.0, H / 2        # large round hole
SMALL_D, SMALL_Y, SMALL_Z = 4.5, 24.0, H / 2  # small round hole

# ---------------- -X wall: LED row ----------------
LED_D = 3.5
LED_Z = 14.1
LED_Y0 = -27.6        # first hole (towards -Y)
LED_PITCH = 5.2
LED_N = 4

# ---------------- floor blind holes ----------------
FLOOR_D = 2.5
FLOOR_DEPTH = 3.0
FLOOR_PTS = [(25.6, 39.9), (25.6, 9.6),          # small board, 2 holes
             (-23.8, -6.6), (10.7, -6.6),         # square board, 4 holes
             (-23.8, -41.4), (10.7, -41.4)]

# =====================================================================
# body: rounded block, hollowed from the top leaving a sharp-cornered cavity
body = (cq.Workplane("XY")
        .box(W, L, H, centered=(True, True, False))
        .edges("|Z").fillet(R_OUT))

cavity = (cq.Workplane("XY").workplane(offset=T_FLOOR)
          .rect(W - 2 * T, L - 2 * T)
          .extrude(H - T_FLOOR + 1.0))
body = body.cut(cavity)

# ---------------- +X wall cut-outs ----------------
def xplus_wp():
    """Workplane just inside the +X wall, normal +X (cuts go outward)."""
    return cq.Workplane("YZ").workplane(offset=W / 2 - T - 1.0)

cut_len = T + 2.0
slot = (xplus_wp()
        .center((SLOT_Y0 + SLOT_Y1) / 2, (SLOT_Z0 + SLOT_Z1) / 2)
        .rect(SLOT_Y1 - SLOT_Y0, SLOT_Z1 - SLOT_Z0)
        .extrude(cut_len))
big = xplus_wp().center(BIG_Y, BIG_Z).circle(BIG_D / 2).extrude(cut_len)
small = xplus_wp().center(SMALL_Y, SMALL_Z).circle(SMALL_D / 2).extrude(cut_len)
body = body.cut(slot).cut(big).cut(small)

# ---------------- -X wall LED holes ----------------
led_pts = [(LED_Y0 + i * LED_PITCH, LED_Z) for i in range(LED_N)]
leds = (cq.Workplane("YZ").workplane(offset=-W / 2 - 1.0)
        .pushPoints(led_pts)
        .circle(LED_D / 2)
        .extrude(cut_len))
body = body.cut(leds)

# ---------------- floor blind holes ----------------
floor_holes = (cq.Workplane("XY").workplane(offset=T_FLOOR - FLOOR_DEPTH)
               .pushPoints(FLOOR_PTS)
               .circle(FLOOR_D / 2)
               .extrude(FLOOR_DEPTH + 1.0))
body = body.cut(floor_holes)

result = body
